import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 150.0          # length along X
W = 100.5          # width along Y
H = 24.8           # height along Z
T = 2.0            # wall thickness
TF = 2.0           # floor thickness
R_V = 1.4          # outer vertical edge radius
R_IN_V = 0.5       # inner vertical corner radius
R_B = 2.0          # outer bottom edge radius
R_IN_FLOOR = 0.75  # inner floor/wall fillet

LIP_W = 0.9        # lid rabbet width (inner part of the wall top)
LIP_D = 1.3        # lid rabbet depth
R_TOP = 0.4        # rounding of the outer top edge

POST_D = 4.8       # standoff diameter
POST_HOLE = 1.7    # standoff pilot hole
POST_TOP = H - 1.6 # standoff top height
COLLAR_H = 2.0     # standoff base collar height
COLLAR_DR = 0.3    # standoff base collar radial flare
POST_C = 3.1       # standoff centre distance from the outer wall face
POST_X = 50.5      # standoffs on front/back walls at x = +-POST_X
POST_Y = 24.5      # standoffs on left/right walls at y = +-POST_Y

SLOT_W = 1.0       # vent slot width
SLOT_H = 12.6      # vent slot height
SLOT_Z = 12.6      # vent slot centre height
SLOT_PITCH = 3.0   # vent slot pitch
SLOT_N = 3         # slots per vent group
VENT_X = (-60.6, -41.1)   # centres of the two vent groups flanking the left standoffs (back wall)
FRONT_VENT_DX = -0.55     # front-wall vent groups sit slightly further towards -X

# back wall (+Y) cut-outs
BK_RECT = (11.2, 5.6)   # w x h
BK_RECT_X = -24.45
BK_RECT_Z = 9.5
BK_CIRC_D = 7.0
BK_CIRC_X = -1.0
BK_CIRC_Z = 12.3

# left wall (-X) cut-outs
LF_RECT = (14.5, 4.7)
LF_RECT_Y = 3.35
LF_RECT_Z = 18.5
LF_CIRC_D = 5.6
LF_CIRC_Y = 15.4
LF_CIRC_Z = 11.1

# ---------------- body ----------------
body = (
    cq.Workplane("XY")
    .rect(L, W)
    .extrude(H)
    .edges("|Z").fillet(R_V)
    .faces("<Z").edges().fillet(R_B)
    .faces(">Z").edges().fillet(R_TOP)
)

# inner cavity
cav = (
    cq.Workplane("XY", origin=(0, 0, TF))
    .rect(L - 2 * T, W - 2 * T)
    .extrude(H)
    .edges("|Z").fillet(R_IN_V)
    .faces("<Z").edges().fillet(R_IN_FLOOR)
)
body = body.cut(cav)

# lid rabbet on the inner half of the rim
rab = (
    cq.Workplane("XY", origin=(0, 0, H - LIP_D))
    .rect(L - 2 * (T - LIP_W), W - 2 * (T - LIP_W))
    .extrude(LIP_D + 1)
    .edges("|Z").fillet(R_IN_V + LIP_W)
)
body = body.cut(rab)

# ---------------- standoffs ----------------
pc = POST_C
post_pts = [
    (POST_X, W / 2 - pc), (-POST_X, W / 2 - pc),
    (POST_X, -W / 2 + pc), (-POST_X, -W / 2 + pc),
    (L / 2 - pc, POST_Y), (L / 2 - pc, -POST_Y),
    (-L / 2 + pc, POST_Y), (-L / 2 + pc, -POST_Y),
]
r = POST_D / 2.0
# one standoff as a revolved profile: column with a slightly flared base collar
post_solid = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(r + COLLAR_DR, 0)
    .lineTo(r, COLLAR_H)
    .lineTo(r, POST_TOP - TF)
    .lineTo(0, POST_TOP - TF)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .val()
)
for (px, py) in post_pts:
    body = body.union(cq.Workplane("XY").add(post_solid.translate(cq.Vector(px, py, TF))))

holes = (
    cq.Workplane("XY", origin=(0, 0, TF + 1.0))
    .pushPoints(post_pts)
    .circle(POST_HOLE / 2.0)
    .extrude(POST_TOP)
)
body = body.cut(holes)

# ---------------- vent slots (front and back walls, around the left standoffs) ----------------
slot_xs = [
    vx + (i - (SLOT_N - 1) / 2.0) * SLOT_PITCH
    for vx in VENT_X
    for i in range(SLOT_N)
]
for ysgn in (1, -1):
    dx = 0.0 if ysgn > 0 else FRONT_VENT_DX
    wp = cq.Workplane("XZ", origin=(dx, ysgn * (W / 2 + 1), 0))
    slots = (
        wp.pushPoints([(x, SLOT_Z) for x in slot_xs])
        .rect(SLOT_W, SLOT_H)
        .extrude(T + 2 if ysgn > 0 else -(T + 2))
    )
    body = body.cut(slots)

# ---------------- back wall cut-outs ----------------
body = body.cut(
    cq.Workplane("XZ", origin=(0, W / 2 + 1, 0))
    .center(BK_RECT_X, BK_RECT_Z).rect(*BK_RECT).extrude(T + 2)
)
body = body.cut(
    cq.Workplane("XZ", origin=(0, W / 2 + 1, 0))
    .center(BK_CIRC_X, BK_CIRC_Z).circle(BK_CIRC_D / 2).extrude(T + 2)
)

# ---------------- left wall cut-outs ----------------
body = body.cut(
    cq.Workplane("YZ", origin=(-L / 2 - 1, 0, 0))
    .center(LF_RECT_Y, LF_RECT_Z).rect(*LF_RECT).extrude(T + 2)
)
body = body.cut(
    cq.Workplane("YZ", origin=(-L / 2 - 1, 0, 0))
    .center(LF_CIRC_Y, LF_CIRC_Z).circle(LF_CIRC_D / 2).extrude(T + 2)
)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
